import cadquery as cq
import math

# ------------------------------------------------------------------
# Ball-ended pawn / knob with a recessed cup base (solid of revolution)
# axis of revolution = global Y ; cup opening faces -Y, ball at +Y
# profile coordinates are (r, y): r = radius, y = axial position
# ------------------------------------------------------------------

# base cup
R_BASE = 20.0        # outer radius of the cup/base
L_BASE = 11.6        # axial length of the base cylinder
R_CUP = 17.27        # inner radius of the cup recess
D_CUP = 9.2          # depth of the cup recess (flat floor)

# first (large) cone stepping off the base
R_STEP = 16.85       # radius where the cone leaves the base shoulder
Y_C1, R_C1 = 15.50, 13.75    # end of the first cone

# cove groove 1 + second cone (ring)
G1_IN = (12.52, 15.50)       # groove 1 entry (after a small radial drop)
G1_BOT = (11.25, 16.92)      # groove 1 deepest point
P1 = (11.85, 18.35)          # sharp ring crest after groove 1
Y_C2, R_C2 = 21.30, 10.18    # end of the second cone

# cove groove 2 leading into the neck
G2_IN = (9.48, 21.30)        # groove 2 entry
G2_BOT = (8.15, 22.80)       # groove 2 deepest point
P2 = (8.92, 24.28)           # crest where the neck starts

# concave neck
NECK_MID = (6.53, 31.40)     # point on the concave neck flank
R_NECK = 5.61                # neck radius where it meets the ball
NECK_FILLET = 1.2            # blend between neck and ball

# ball
BALL_Y = 47.36       # ball centre on the axis
BALL_R = 9.95        # ball radius

# ------------------------------------------------------------------
ball_tip = BALL_Y + BALL_R
neck_y_ball = BALL_Y - math.sqrt(BALL_R ** 2 - R_NECK ** 2)
ball_mid = (BALL_R * math.sin(math.radians(60)),
            BALL_Y + BALL_R * math.cos(math.radians(60)))

# half profile drawn in the XY plane (X = radius, Y = axial)
prof = (
    cq.Workplane("XY")
    .moveTo(0, D_CUP)                 # cup floor centre
    .lineTo(R_CUP, D_CUP)             # cup floor
    .lineTo(R_CUP, 0)                 # cup inner wall
    .lineTo(R_BASE, 0)                # rim face
    .lineTo(R_BASE, L_BASE)           # base outer cylinder
    .lineTo(R_STEP, L_BASE)           # shoulder
    .lineTo(R_C1, Y_C1)               # first cone
    .lineTo(*G1_IN)                   # small drop into groove 1
    .threePointArc(G1_BOT, P1)        # groove 1 (cove)
    .lineTo(R_C2, Y_C2)               # second cone
    .lineTo(*G2_IN)                   # small drop into groove 2
    .threePointArc(G2_BOT, P2)        # groove 2 (cove)
    .threePointArc(NECK_MID, (R_NECK, neck_y_ball))   # concave neck
    .threePointArc(ball_mid, (0, ball_tip))           # ball
    .close()
)

body = prof.revolve(360, (0, 0, 0), (0, 1, 0))

# soft blend where the neck meets the ball
tol = 0.2
body = body.edges(
    cq.selectors.BoxSelector((-R_NECK - tol, neck_y_ball - tol, -R_NECK - tol),
                             (R_NECK + tol, neck_y_ball + tol, R_NECK + tol))
).fillet(NECK_FILLET)

# turn the revolve seam to the underside (cosmetic only)
result = body.rotate((0, 0, 0), (0, 1, 0), 90)

VIEW = {"azimuth": 45, "elevation": 26}
